import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 240.0      # length of enclosure along Y
H = 140.0      # height of the (open) back side
HF = 70.0      # height of the front (slotted) wall
D = 60.5       # depth along X (back plane at x=0, front wall at x=D)
T = 2.0        # sheet thickness

RIM_TB = 13.0  # height of the top / bottom back flange (closed by a shelf)

# vent slots in front wall
SLOT_N = 36
SLOT_PITCH = 6.05
SLOT_W = 3.0
SLOT_LEN = 25.0
SLOT_Y0 = -L / 2 + 12.0

# horizontal counterbored screw holes (through back flange, pocket in slope)
HANG_Y = [-83.0, 0.0, 83.0]
HANG_Z = H / 2 - 7.5
HANG_R_SMALL = 2.0
HANG_R_BIG = 4.2
HANG_CB_X = 7.7      # x where the counterbore (pocket floor) starts

# +Y end wall: notch at back edge and 4 cable holes
NOTCH_DEPTH = 22.5
NOTCH_H = 40.0
NOTCH_ZC = 0.0
EH_N = 4
EH_D = 6.5
EH_PITCH = 12.0
EH_X = 34.0
END_EDGE_R = 1.5     # small round on the outer edges of the +Y end face

# internal standoffs (along X, from front wall towards the back opening)
BIG_SO_D = 13.0
BIG_SO_HOLE = 4.0
BIG_SO_END_X = 1.0
BIG_SO_POS = [(86.0, 33.0), (-62.0, 34.5), (-70.0, -37.0), (86.0, -44.0)]

SMALL_SO_D = 7.5
SMALL_SO_HOLE = 2.5
SMALL_SO_LEN = 19.0
SMALL_SO_Y = [57.5, 20.0, -17.5]
SMALL_SO_Z = [15.0, -15.0]

# ---------------- body ----------------
profile = [(0.0, -H / 2), (D, -HF / 2), (D, HF / 2), (0.0, H / 2)]


def envelope():
    return (
        cq.Workplane("XZ")
        .polyline(profile)
        .close()
        .extrude(L / 2, both=True)
    )


env = envelope()
body = env.faces("<X").shell(-T)

# top and bottom back flanges, closed by a horizontal shelf (solid wedge)
zr = H / 2 - RIM_TB
top_band = cq.Workplane("XY").box(D + 2, L + 2, RIM_TB + 1, centered=(False, True, False)) \
    .translate((-1, 0, zr))
bot_band = cq.Workplane("XY").box(D + 2, L + 2, RIM_TB + 1, centered=(False, True, False)) \
    .translate((-1, 0, -H / 2 - 1))
wedges = env.intersect(top_band.union(bot_band))
body = body.union(wedges)

# vent slots on the front wall
slot_pts = [(SLOT_Y0 + i * SLOT_PITCH, 0.0) for i in range(SLOT_N)]
slots = (
    cq.Workplane("YZ", origin=(D - 3 * T, 0, 0))
    .pushPoints(slot_pts)
    .slot2D(SLOT_LEN, SLOT_W, angle=90)
    .extrude(6 * T)
)
body = body.cut(slots)

# screw holes along X (top and bottom) with access pocket in sloped wall
for zs in (1, -1):
    for y in HANG_Y:
        small = (
            cq.Workplane("YZ", origin=(-5.0, 0, 0))
            .center(y, zs * HANG_Z)
            .circle(HANG_R_SMALL)
            .extrude(HANG_CB_X + 6)
        )
        big = (
            cq.Workplane("YZ", origin=(HANG_CB_X, 0, 0))
            .center(y, zs * HANG_Z)
            .circle(HANG_R_BIG)
            .extrude(D)
        )
        body = body.cut(small).cut(big)

# notch in the back edge of the +Y end wall
notch = (
    cq.Workplane("XY")
    .box(NOTCH_DEPTH + 1, T + 2, NOTCH_H, centered=(False, True, True))
    .translate((-1.0, L / 2 - T / 2, NOTCH_ZC))
)
body = body.cut(notch)
body = body.clean()
body = body.faces(">Y").edges().fillet(END_EDGE_R)

# cable holes in the +Y end wall
eh_pts = [(EH_X, NOTCH_ZC + (i - (EH_N - 1) / 2) * EH_PITCH) for i in range(EH_N)]
eholes = (
    cq.Workplane("XZ", origin=(0, L / 2 + 1, 0))
    .pushPoints(eh_pts)
    .circle(EH_D / 2)
    .extrude(T + 2)
)
body = body.cut(eholes)

# large standoffs: from front wall back to near the open back plane
big_so = None
for (y, z) in BIG_SO_POS:
    c = (
        cq.Workplane("YZ", origin=(BIG_SO_END_X, 0, 0))
        .center(y, z)
        .circle(BIG_SO_D / 2)
        .extrude(D - BIG_SO_END_X)
    )
    big_so = c if big_so is None else big_so.union(c)
big_so = big_so.intersect(env)
body = body.union(big_so)
for (y, z) in BIG_SO_POS:
    h = (
        cq.Workplane("YZ", origin=(BIG_SO_END_X - 1, 0, 0))
        .center(y, z)
        .circle(BIG_SO_HOLE / 2)
        .extrude(10.0)
    )
    body = body.cut(h)

# small studs pressed into the inside of the front wall
small_pts = [(y, z) for y in SMALL_SO_Y for z in SMALL_SO_Z]
x_in = D - T
studs = (
    cq.Workplane("YZ", origin=(x_in - SMALL_SO_LEN, 0, 0))
    .pushPoints(small_pts)
    .circle(SMALL_SO_D / 2)
    .extrude(SMALL_SO_LEN + 0.5)
)
body = body.union(studs)
stud_holes = (
    cq.Workplane("YZ", origin=(x_in - SMALL_SO_LEN - 1, 0, 0))
    .pushPoints(small_pts)
    .circle(SMALL_SO_HOLE / 2)
    .extrude(8.0)
)
body = body.cut(stud_holes)

result = body
